import cadquery as cq
import math

# ---------------- driving dimensions (mm) ----------------
W = 26.0            # overall depth (Y), front at Y=0, back at Y=W
RAIL_D = 12.0       # depth of the front rails
RAIL_H = 7.6        # height of the front rails
RAIL_CH = 2.7       # chamfer on rail top/front edge
CH_EDGE_R = 1.1     # soft edges of the rail chamfer
RAIL_END_R = 1.2    # fillet on front corner of the right rail inner end
RAIL_END_RL = 1.2   # same for the left rail inner end
BLEND_R = 1.0       # blend of the right rail end into the sloped plate
R_END_TOP_R = 1.5   # rounded top edge at the inner end of the right rail
TAB_R = 0.5         # vertical corner fillet on left wedge
RIDGE_R = 1.0       # ramp/rail-top ridge fillet
CORNER_R = 0.8      # ramp / corner-cut edge fillet

# left end (rising ramp + wedge)
XL_TAB = 19.05      # x of vertical +X face of left wedge
ZL_TOP = 14.65      # top of left wedge
L_CHAMF = 9.8       # 45 deg corner cut at front-left (X+Y >= L_CHAMF)
XL_RAIL_END = 35.7  # end ridge of left rail (top edge of its sloped end)
L_END_RUN = 2.8     # horizontal run of the sloped end face of the left rail
NOTCH_X0 = 22.7     # notch through left rail
NOTCH_Y0 = 4.55
SMALL_HOLE_D = 2.0
SMALL_HOLE_X = (25.85, 32.0)
SMALL_HOLE_Z = 2.7
LH_Y = 18.7         # axis of the X-direction hole in left wedge
LH_Z = 7.8
LH_D = 3.25
LH_CB_D = 6.0
LH_CB_DEPTH = 16.0  # counterbore depth measured from x=0 along +X

# central sloped plate
XP0 = 33.55
XP1 = 84.85
ZP_BACK_TOP = 16.6
ZP_BACK_BOT = 14.5
ZP_FRONT = 0.15
YP_UNDER = 12.0     # underside meets the ground here
BOSS_X = 59.2
BOSS_Y = 16.45
BOSS_OD = 15.0
BOSS_ID = 9.6
BOSS_TOP = 16.65
BOSS_TOP_R = 2.0
BOSS_BASE_R = 2.0

# right end (rail + descending ramp)
XR_RAIL0 = 82.55    # top edge of the sloped inner end of the right rail
R_END_RUN = 2.7
XR_RAMP0 = 109.0
X_END = 118.5
Z_END = 0.4
RH_X = 92.0
RH_Z = 3.3
RH_CB_D = 6.3
RH_CB_DEPTH = 5.0
RH_D = 3.0


def prism_xz(pts, y0, y1):
    """polygon in XZ extruded from y0 to y1"""
    return (cq.Workplane("XZ", origin=(0, y0, 0)).polyline(pts).close()
            .extrude(-(y1 - y0)))


def prism_yz(pts, x0, x1):
    """polygon in YZ extruded from x0 to x1"""
    return (cq.Workplane("YZ", origin=(x0, 0, 0)).polyline(pts).close()
            .extrude(x1 - x0))


def prism_xy(pts, z0, z1):
    return (cq.Workplane("XY", origin=(0, 0, z0)).polyline(pts).close()
            .extrude(z1 - z0))


# ---------------- left end ----------------
slopeL = ZL_TOP / XL_TAB
x_rail_ramp = RAIL_H / slopeL
left_rail = prism_xz([(0, 0), (XL_RAIL_END + L_END_RUN, 0), (XL_RAIL_END, RAIL_H),
                      (x_rail_ramp, RAIL_H)], 0, RAIL_D)
left_wedge = prism_xz([(0, 0), (XL_TAB, 0), (XL_TAB, ZL_TOP)], RAIL_D, W)
left = left_rail.union(left_wedge)
# 45 deg corner cut
left = left.cut(prism_xy([(-1, -1), (L_CHAMF + 1, -1), (-1, L_CHAMF + 1)], -1, 50))

# ---------------- central plate ----------------
plate = prism_yz([(0, 0), (0, ZP_FRONT), (W, ZP_BACK_TOP), (W, ZP_BACK_BOT),
                  (YP_UNDER, 0)], XP0, XP1)
boss = (cq.Workplane("XY").center(BOSS_X, BOSS_Y).circle(BOSS_OD / 2)
        .extrude(BOSS_TOP))
boss = boss.faces(">Z").edges().fillet(BOSS_TOP_R)
# keep boss only above the plate underside
slope_u = ZP_BACK_BOT / (W - YP_UNDER)
above_under = prism_yz([(-5, -1), (YP_UNDER - 1 / slope_u, -1),
                        (W + 5, ZP_BACK_BOT + 5 * slope_u), (W + 5, 50), (-5, 50)],
                       XP0 - 5, XP1 + 5)
boss = boss.intersect(above_under)
plate = plate.union(boss)


def _on_plate_top(p):
    z = ZP_FRONT + (ZP_BACK_TOP - ZP_FRONT) * p.y / W
    return abs(p.z - z) < 1e-3


base_edges = []
for e in plate.edges().vals():
    pts = [e.positionAt(t) for t in (0.0, 0.3, 0.6, 1.0)]
    if all(_on_plate_top(p) and
           abs(math.hypot(p.x - BOSS_X, p.y - BOSS_Y) - BOSS_OD / 2) < 1e-3
           for p in pts):
        base_edges.append(e)
if base_edges:
    plate = plate.newObject(base_edges).fillet(BOSS_BASE_R)
plate = plate.cut(cq.Workplane("XY").center(BOSS_X, BOSS_Y).circle(BOSS_ID / 2)
                  .extrude(60).translate((0, 0, -20)))

# ---------------- right end ----------------
right_rail = prism_xz([(XR_RAIL0 - R_END_RUN, 0), (X_END, 0), (X_END, Z_END),
                       (XR_RAMP0, RAIL_H), (XR_RAIL0, RAIL_H)], 0, RAIL_D)
right_wedge = prism_xz([(XR_RAMP0, 0), (X_END, 0), (X_END, Z_END),
                        (XR_RAMP0, RAIL_H)], RAIL_D, W)
right = right_rail.union(right_wedge)
# 45 deg corner cut at front-right (keep X - Y <= XR_RAMP0)
right = right.cut(prism_xy([(XR_RAMP0 - 1, -1), (X_END + 5, -1),
                            (X_END + 5, X_END + 5 - XR_RAMP0)], -1, 50))

# rail top-front chamfer (45 deg, cut along the rails only)
def rail_chamfer(x0, x1):
    zc = RAIL_H - RAIL_CH
    return prism_yz([(-1, zc - 1), (-1, 60), (60 - zc, 60)], x0, x1)


left = left.cut(rail_chamfer(-5, XL_RAIL_END + L_END_RUN + 1))
right = right.cut(rail_chamfer(XR_RAIL0 - R_END_RUN - 1, X_END + 5))

body = left.union(plate).union(right)
# notch through the left rail (also trims the plate corner)
body = body.cut(prism_xy([(NOTCH_X0, NOTCH_Y0), (XL_RAIL_END, NOTCH_Y0),
                          (XL_RAIL_END, RAIL_D + 1), (NOTCH_X0, RAIL_D + 1)],
                         -1, 50))

# ---------------- holes ----------------
# small holes through left rail front into the notch
def y_hole(x, z, d, depth):
    """hole along +Y starting in front of the part (y<0)"""
    return (cq.Workplane("XZ", origin=(0, -1, 0)).center(x, z).circle(d / 2)
            .extrude(-(depth + 1)))


for hx in SMALL_HOLE_X:
    body = body.cut(y_hole(hx, SMALL_HOLE_Z, SMALL_HOLE_D, NOTCH_Y0 + 1))
# X-direction counterbored hole in the left wedge (counterbore from ramp side)
body = body.cut(cq.Workplane("YZ", origin=(-1, 0, 0)).center(LH_Y, LH_Z)
                .circle(LH_D / 2).extrude(XL_TAB + 5))
body = body.cut(cq.Workplane("YZ", origin=(-1, 0, 0)).center(LH_Y, LH_Z)
                .circle(LH_CB_D / 2).extrude(LH_CB_DEPTH + 1))
# counterbored hole through the right rail (front to back)
body = body.cut(y_hole(RH_X, RH_Z, RH_CB_D, RH_CB_DEPTH))
body = body.cut(y_hole(RH_X, RH_Z, RH_D, RAIL_D + 2))

# ---------------- edge treatment ----------------
def edges_where(wp, pred, ts=(0.0, 0.5, 1.0)):
    out = []
    for e in wp.edges().vals():
        if all(pred(e.positionAt(t)) for t in ts):
            out.append(e)
    return out


def try_fillet(wp, pred, r):
    es = edges_where(wp, pred)
    if not es:
        return wp
    try:
        res = wp.newObject(es).fillet(r)
        if res.val().isValid():
            return res
    except Exception:
        pass
    return wp


EPS = 1e-3


def z_plate(y):
    return ZP_FRONT + (ZP_BACK_TOP - ZP_FRONT) * y / W


def on_left_end(p):
    return abs(p.z - (RAIL_H - (p.x - XL_RAIL_END) * RAIL_H / L_END_RUN)) < EPS


def on_right_end(p):
    return abs(p.z - (RAIL_H - (XR_RAIL0 - p.x) * RAIL_H / R_END_RUN)) < EPS


# right rail: rounded top edge of the sloped inner end
body = try_fillet(body, lambda p: abs(p.x - XR_RAIL0) < EPS and
                  p.z > RAIL_H - RAIL_CH - EPS and
                  (abs(p.z - RAIL_H) < EPS or abs(p.z - (RAIL_H - RAIL_CH + p.y)) < EPS),
                  R_END_TOP_R)
# front corners of the sloped rail ends
body = try_fillet(body, lambda p: abs(p.y) < EPS and on_right_end(p), RAIL_END_R)
body = try_fillet(body, lambda p: abs(p.y) < EPS and on_left_end(p), RAIL_END_RL)
# blend of the right rail sloped end into the plate
body = try_fillet(body, lambda p: on_right_end(p) and abs(p.z - z_plate(p.y)) < EPS,
                  BLEND_R)
# soften both edges of the rail top/front chamfer
_zc = RAIL_H - RAIL_CH
body = try_fillet(body, lambda p: (abs(p.y - RAIL_CH) < EPS and abs(p.z - RAIL_H) < EPS)
                  or (abs(p.y) < EPS and abs(p.z - _zc) < EPS), CH_EDGE_R)
# vertical corner of the left wedge and the ramp/rail ridge
body = try_fillet(body, lambda p: abs(p.x - XL_TAB) < EPS and
                  abs(p.y - RAIL_D) < EPS and p.z > RAIL_H - EPS, TAB_R)
body = try_fillet(body, lambda p: abs(p.x - x_rail_ramp) < 0.05 and
                  abs(p.z - RAIL_H) < EPS, RIDGE_R)

# soften the ramp / 45 deg corner-cut edge at the far left
body = try_fillet(body, lambda p: abs(p.x + p.y - L_CHAMF) < EPS and
                  abs(p.z - slopeL * p.x) < EPS, CORNER_R)

result = body
